import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
L = 130.0          # overall length along X
W = 106.0          # overall width along Y
H = 80.0           # overall height along Z
R_OUT = 2.0        # outer radius of the vertical corners
T = 3.9            # wall thickness
TF = 3.6           # floor thickness (top of floor above the base)

# semicircular cradle cut-outs (centres on the top edge)
R_FRONT = 54.7     # in the front/back walls (XZ plane)
R_SIDE = 50.45     # in the left/right walls (YZ plane); also bevels the
                   # inner top edge of the front/back wall ends

# side wall holes (one per side wall, point-symmetric)
SIDE_HOLE_D = 3.6
SIDE_HOLE_Y = 32.0
SIDE_HOLE_Z = 18.0

# mounting posts
POST_X = 38.1
POST_Y = 24.7
POST_S = 12.2
POST_TOP = 30.3    # top of posts above the base
POST_TFIL = 1.0
POST_HOLE_D = 2.5
POST_CSK_D = 6.0
POST_HOLE_DEPTH = 12.0

# central raised pad with a rectangular window
PAD_L = 29.6       # along X
PAD_W = 55.4       # along Y
PAD_TOP = 11.8     # top of the pad above the base
PAD_VFIL = 1.0
PAD_TFIL = 0.8
WIN_L = 18.2
WIN_W = 37.0
PAD_HOLE_Y = 22.4
PAD_HOLE_D = 2.0
PAD_CSK_D = 4.2

# ---------------- shell (walls + floor) ----------------

outer = (cq.Workplane("XY").rect(L, W).extrude(H)
         .edges("|Z").fillet(R_OUT))

# open-topped cavity
cavity = (cq.Workplane("XY").workplane(offset=TF)
          .rect(L - 2 * T, W - 2 * T)
          .extrude(H))
body = outer.cut(cavity)

# cradle cut-outs in front/back walls (cylinder axis along Y)
cyl_front = (cq.Workplane("XZ").workplane(offset=-W)
             .center(0, H).circle(R_FRONT).extrude(2 * W))
# cradle cut-outs in side walls (cylinder axis along X)
cyl_side = (cq.Workplane("YZ").workplane(offset=-L)
            .center(0, H).circle(R_SIDE).extrude(2 * L))
body = body.cut(cyl_front).cut(cyl_side)

# small holes in the side walls
hole_r = (cq.Workplane("YZ").workplane(offset=L / 2 - 8.0)
          .center(-SIDE_HOLE_Y, SIDE_HOLE_Z).circle(SIDE_HOLE_D / 2).extrude(10.0))
hole_l = (cq.Workplane("YZ").workplane(offset=-L / 2 - 2.0)
          .center(SIDE_HOLE_Y, SIDE_HOLE_Z).circle(SIDE_HOLE_D / 2).extrude(10.0))
body = body.cut(hole_r).cut(hole_l)

# ---------------- mounting posts ----------------
post_pts = [(sx * POST_X, sy * POST_Y) for sx in (-1, 1) for sy in (-1, 1)]
post = (cq.Workplane("XY").workplane(offset=TF - 0.5)
        .rect(POST_S, POST_S).extrude(POST_TOP - TF + 0.5)
        .faces(">Z").edges().fillet(POST_TFIL))
for px, py in post_pts:
    body = body.union(post.translate((px, py, 0)))
body = (body.faces(cq.selectors.NearestToPointSelector((POST_X, POST_Y, POST_TOP + 5)))
        .workplane(centerOption="ProjectedOrigin", origin=(0, 0, 0))
        .pushPoints(post_pts)
        .cskHole(POST_HOLE_D, POST_CSK_D, 90, depth=POST_HOLE_DEPTH))

# ---------------- central pad with window ----------------
pad = (cq.Workplane("XY").workplane(offset=TF - 0.5)
       .rect(PAD_L, PAD_W).extrude(PAD_TOP - TF + 0.5)
       .edges("|Z").fillet(PAD_VFIL)
       .faces(">Z").edges().fillet(PAD_TFIL))
body = body.union(pad)
body = (body.faces(cq.selectors.NearestToPointSelector((0, 0, PAD_TOP + 0.5)))
        .workplane(centerOption="ProjectedOrigin", origin=(0, 0, 0))
        .pushPoints([(0, PAD_HOLE_Y), (0, -PAD_HOLE_Y)])
        .cskHole(PAD_HOLE_D, PAD_CSK_D, 90, depth=PAD_TOP - TF))
window = (cq.Workplane("XY").workplane(offset=-1)
          .rect(WIN_L, WIN_W).extrude(PAD_TOP + 2))
body = body.cut(window)

result = body

VIEW = {"azimuth": 45, "elevation": 26}
